import cadquery as cq
import math

# =====================================================================
#  Twisted three-bar cage between two end caps
#  (axis along +Y; thin -Y cap with a plain bore, thick +Y cap with a
#   bore and eight square blind pockets on its outer face)
# =====================================================================

# ---------------- overall / caps (mm) ----------------
L_total   = 252.0   # overall length along Y
D_cap     = 40.0    # end cap diameter
T_cap0    = 6.0     # -Y end cap thickness
T_cap1    = 11.4    # +Y end cap thickness
D_hole0   = 11.6    # central through bore, -Y cap
D_hole1   = 12.0    # central through bore, +Y cap

# ---------------- twisted bars ----------------
n_bar     = 3       # number of bars (equally spaced)
R_out     = 19.2    # outer radius of the bars
t_bar     = 1.6     # radial thickness of the bars (long edges fully rounded)
w_bar     = 70.6    # angular width of each bar (deg, over the rounded ends)
phi0      = 22.5    # centre angle of the first bar at the -Y end
                    # (XZ plane, measured from +X toward +Z)
twist     = -57.0   # helical twist from the -Y end to the +Y end (deg about +Y)

# ---------------- square pockets on the +Y cap ----------------
n_sq      = 8
r_sq      = 12.5    # pitch radius of the pockets
a_sq      = 6.0     # pocket side length
d_sq      = 2.0     # pocket depth

# ---------------- derived ----------------
L_rotor   = L_total - T_cap0 - T_cap1
R_mid     = R_out - t_bar / 2
h         = t_bar / 2
half_core = w_bar / 2 - math.degrees(h / R_mid)   # half angle between end-round centres


def P(r, ang_deg, y):
    a = math.radians(ang_deg)
    return cq.Vector(r * math.cos(a), y, r * math.sin(a))


def bar_profile(phi_deg, y):
    """Arc-slot cross section (annular sector with full-round ends) in the plane Y=y."""
    a0 = phi_deg - half_core
    a1 = phi_deg + half_core
    c0 = P(R_mid, a0, y)
    c1 = P(R_mid, a1, y)
    t0 = cq.Vector(-math.sin(math.radians(a0)), 0, math.cos(math.radians(a0)))
    t1 = cq.Vector(-math.sin(math.radians(a1)), 0, math.cos(math.radians(a1)))
    e_out = cq.Edge.makeThreePointArc(P(R_out, a0, y), P(R_out, phi_deg, y), P(R_out, a1, y))
    e_end1 = cq.Edge.makeThreePointArc(P(R_out, a1, y), c1 + t1 * h, P(R_mid - h, a1, y))
    e_in = cq.Edge.makeThreePointArc(P(R_mid - h, a1, y), P(R_mid - h, phi_deg, y), P(R_mid - h, a0, y))
    e_end0 = cq.Edge.makeThreePointArc(P(R_mid - h, a0, y), c0 - t0 * h, P(R_out, a0, y))
    return cq.Wire.assembleEdges([e_out, e_end1, e_in, e_end0])


# straight spine along the axis + auxiliary helix that drives the twist
spine = cq.Wire.assembleEdges(
    [cq.Edge.makeLine(cq.Vector(0, T_cap0, 0), cq.Vector(0, T_cap0 + L_rotor, 0))])
aux_helix = cq.Wire.makeHelix(360.0 / abs(twist) * L_rotor, L_rotor, 1.0,
                              center=cq.Vector(0, T_cap0, 0), dir=cq.Vector(0, 1, 0),
                              lefthand=(twist > 0))


def twisted_bar(phi_deg):
    prof = bar_profile(phi_deg, T_cap0)
    return cq.Solid.sweep(prof, [], spine, makeSolid=True, isFrenet=False, mode=aux_helix)


bars = cq.Workplane("XY")
for k in range(n_bar):
    bars = bars.union(cq.Workplane("XY").add(twisted_bar(phi0 + 360.0 / n_bar * k)))

# -Y end cap (Y = 0 .. T_cap0)
cap0 = (cq.Workplane("XZ")
        .circle(D_cap / 2).circle(D_hole0 / 2)
        .extrude(-T_cap0))

# +Y end cap (Y = L_total - T_cap1 .. L_total)
cap1 = (cq.Workplane("XZ").workplane(offset=-(L_total - T_cap1))
        .circle(D_cap / 2).circle(D_hole1 / 2)
        .extrude(-T_cap1))

# eight square blind pockets on the outer (+Y) face of the +Y cap
pockets = None
for k in range(n_sq):
    ang = 360.0 / n_sq * k
    p = (cq.Workplane("XZ").workplane(offset=-(L_total - d_sq))
         .transformed(rotate=(0, 0, ang))
         .center(r_sq, 0).rect(a_sq, a_sq)
         .extrude(-(d_sq + 1.0)))
    pockets = p if pockets is None else pockets.union(p)
cap1 = cap1.cut(pockets)

result = cap0.union(bars).union(cap1)
